import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length along X
W = 71.3           # overall width along Y
H = 22.15          # overall height along Z

CORNER_CH = 9.2   # plan-view corner chamfer (leg length)
CORNER_R = 7.0     # fillet radius at chamfer/edge transitions

TOP_CH = 2.0       # chamfer on top perimeter edges
BOT_CH = 3.0       # chamfer on bottom perimeter edges

CH_W = 43.4        # channel (slot) width along X
CH_D = 2.9         # channel depth
CH_X = -4.6        # channel centre offset along X

HOLE_D = 16.2      # through hole diameter
HOLE_PITCH = 56.9  # hole centre distance (along X)
HOLE_TOP_CH = 2.0  # 45 deg countersink at top of hole
HOLE_BOT_CH = 2.0  # 45 deg chamfer at bottom of hole
NOTCH_CH = 2.0     # chamfer on the vertical edges where a hole breaks a channel wall

VIEW = {"azimuth": 45, "elevation": 26}


def plan_sketch():
    hx, hy, c = L / 2.0, W / 2.0, CORNER_CH
    pts = [
        (-hx + c, -hy), (hx - c, -hy), (hx, -hy + c), (hx, hy - c),
        (hx - c, hy), (-hx + c, hy), (-hx, hy - c), (-hx, -hy + c),
    ]
    return cq.Sketch().polygon(pts + [pts[0]]).vertices().fillet(CORNER_R)


def slab(height):
    s = cq.Workplane("XY").placeSketch(plan_sketch()).extrude(height)
    s = s.faces(">Z").edges().chamfer(TOP_CH)
    s = s.faces("<Z").edges().chamfer(BOT_CH)
    return s


# full-height body and the lower body that forms the channel floor
body_full = slab(H)
body_low = slab(H - CH_D)

# channel region: keep only the lower body inside the slot band
band = (
    cq.Workplane("XY")
    .box(CH_W, W + 20.0, H + 10.0, centered=(True, True, False))
    .translate((CH_X, 0, -2.0))
)
part = body_full.cut(band.cut(body_low))

# plain through holes
r = HOLE_D / 2.0
hole_x = [CH_X - HOLE_PITCH / 2.0, CH_X + HOLE_PITCH / 2.0]
for hx in hole_x:
    part = part.cut(
        cq.Workplane("XY").circle(r).extrude(H + 2.0).translate((hx, 0, -1.0))
    )

# chamfer the vertical edges where the holes break through the channel walls
wall_x = [CH_X - CH_W / 2.0, CH_X + CH_W / 2.0]
notch_edges = []
for edge in part.edges().vals():
    if edge.geomType() != "LINE":
        continue
    a, b = edge.startPoint(), edge.endPoint()
    vertical = abs(a.x - b.x) < 1e-6 and abs(a.y - b.y) < 1e-6
    on_wall = any(abs(a.x - xw) < 1e-3 for xw in wall_x)
    if vertical and on_wall and abs(a.y) < r:
        notch_edges.append(edge)
if notch_edges and NOTCH_CH > 0:
    part = part.newObject(notch_edges).chamfer(NOTCH_CH)

# 45 deg countersink at the top and chamfer at the bottom of each hole
e = 1.0
top_cone = (
    cq.Workplane("XZ")
    .polyline([(0, H - HOLE_TOP_CH), (r, H - HOLE_TOP_CH),
               (r + HOLE_TOP_CH + e, H + e), (0, H + e)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
bot_cone = (
    cq.Workplane("XZ")
    .polyline([(0, -e), (r + HOLE_BOT_CH + e, -e), (r, HOLE_BOT_CH), (0, HOLE_BOT_CH)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
for hx in hole_x:
    part = part.cut(top_cone.translate((hx, 0, 0)))
    part = part.cut(bot_cone.translate((hx, 0, 0)))

result = part
